"""Saddle bracket: central body with a half-round saddle opening toward +X, a holed tab
toward -X, and two curved spring-like arms along +/-Y ending in bored bosses.

Frame: X from the tab end toward the saddle, Y along the arms, Z up.  The finished part is
tilted slightly about Y, as it sits in the reference.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# tab / keel
TAB_L = 12.65        # tab length before the body step
TAB_HW = 6.7         # tab (and keel) half width in Y
TAB_H = 10.75        # tab height
TAB_R = 1.7          # rounding of the tab end edges
TAB_HOLE_X = 5.6     # cross hole (along Y) through the tab
TAB_HOLE_Z = 5.6
TAB_HOLE_R = 2.22
KEEL_LEN = 45.0      # keel runs under the body up to the saddle
KEEL_FILLET = 1.5    # concave rounding where the keel meets the body underside

# central body
BODY_TOP = 15.9      # top of the central body
BODY_BOT = 6.5       # underside of the body outside the keel
BODY_XMAX = 52.0     # body extends to here before the saddle cut
UNDER_Z0 = 2.0       # underside slope starts at this height at the body step
# two concave scallops per side (top view, +Y side): start / mid / end points
SCALLOPS = [
    ((TAB_L, TAB_HW), (19.5, 9.2), (24.3, 15.68)),
    ((24.3, 15.68), (30.8, 18.95), (36.35, 25.32)),
]
LEDGE_W = 1.3        # bead at the foot of the second scallop
LEDGE_TOP = 10.75

# saddle (half-round opening toward +X)
SADDLE_CX = 59.8
SADDLE_R = 25.1
LIP_A0 = 54.0        # thin lips on the upper saddle edge: angular span from -X
LIP_A1 = 73.0
LIP_W = 1.5          # radial protrusion of a lip
LIP_T = 1.5          # lip thickness

# arms
ARM_X0 = 36.05       # inner (-X) edge of the arm lobes
ARM_Y0 = 18.0        # arm start (buried in the body)
ARM_LEN = 59.1       # half length of the part (tip of the lobes)
# closed cross-section of the curved arm band (X-Z), extruded along Y and trimmed by the
# lobe outline; the loop beyond X = LOBE_XMAX is cut away by the lobe wall
ARM_SECTION = [
    (62.0, 20.2), (57.0, 19.6), (52.9, 19.3), (47.75, 18.2), (42.4, 15.75), (38.8, 12.5),
    (36.7, 9.7), (36.3, 8.0), (37.5, 6.9), (40.3, 6.9), (44.0, 8.25), (47.35, 10.2),
    (52.1, 12.1), (56.8, 13.3), (62.0, 14.0), (63.5, 17.0),
]
ARM_RIM_FILLET = 3.0
LOBE_CLEAR = 0.45     # inner lobe wall sits just outside the band's nose
LOBE_TIP_R = 8.0      # lobe tip corner rounding, inner side
LOBE_OUT_R = 7.0      # lobe tip corner rounding, outer side
LOBE_XMAX = 57.0      # outermost X of the lobe
LOBE_P1 = (54.5, 33.1)  # outer edge of the lobe curves in through this point ...
LOBE_X_END = 46.0       # ... and reaches this X at the arm start
TAPER_CY = 39.0       # rounded shoulder lowering the arm top toward the body:
TAPER_CZ = -17.35     # circle (in YZ) centre and radius, its top at Z = 19.9
TAPER_R = 37.25
TAPER_FILLET = 2.0

# block under each arm
BLOCK_X0 = 37.2
BLOCK_X1 = 52.0
BLOCK_Y0 = 23.8
BLOCK_Y1 = 49.25
BLOCK_TOP = 15.9     # buried inside the band

# bosses at the arm tips
BOSS_X = 46.5
BOSS_Y = 53.9
BOSS_R = 4.35
BOSS_BASE = 12.0     # boss cylinder starts inside the band
BOSS_TOP = 24.15
BOSS_HOLE_R = 2.5
CB_R = 4.0           # counterbore from below into the band at the tip
CB_TOP = 12.5

TILT_DEG = -2.5      # the whole part sits slightly rotated about Y

BIG = 200.0


# ---------------- helpers ----------------
def circle_through(p1, p2, p3):
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    d = 2 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    cx = ((x1**2 + y1**2) * (y2 - y3) + (x2**2 + y2**2) * (y3 - y1) + (x3**2 + y3**2) * (y1 - y2)) / d
    cy = ((x1**2 + y1**2) * (x3 - x2) + (x2**2 + y2**2) * (x1 - x3) + (x3**2 + y3**2) * (x2 - x1)) / d
    return cx, cy, math.hypot(x1 - cx, y1 - cy)


def annular_sector(cx, cy, r_in, r_out, a0, a1, flip_y=False):
    """closed wire of a ring sector on XY (angles in radians, measured at (cx, cy))"""
    s = -1.0 if flip_y else 1.0

    def pt(r, a):
        return (cx + r * math.cos(a), s * (cy + r * math.sin(a)))

    am = 0.5 * (a0 + a1)
    return (
        cq.Workplane("XY")
        .moveTo(*pt(r_out, a0))
        .lineTo(*pt(r_in, a0))
        .threePointArc(pt(r_in, am), pt(r_in, a1))
        .lineTo(*pt(r_out, a1))
        .threePointArc(pt(r_out, am), pt(r_out, a0))
        .close()
    )


# ---------------- keel + tab ----------------
keel = cq.Workplane("XY").box(KEEL_LEN, 2 * TAB_HW, TAB_H, centered=(False, True, False))
keel = keel.edges("|Y and <X").fillet(TAB_R)


# ---------------- body (flared outline) ----------------
def body_profile():
    ye = SCALLOPS[-1][2][1]
    w = cq.Workplane("XY").moveTo(TAB_L, -TAB_HW).lineTo(TAB_L, TAB_HW)
    for _, m, e in SCALLOPS:
        w = w.threePointArc(m, e)
    w = w.lineTo(BODY_XMAX, ye).lineTo(BODY_XMAX, -ye)
    w = w.lineTo(SCALLOPS[-1][2][0], -ye)
    for s_, m, _ in reversed(SCALLOPS):
        w = w.threePointArc((m[0], -m[1]), (s_[0], -s_[1]))
    return w.close()


body = body_profile().extrude(BODY_TOP)
# underside rises from near the keel bottom to BODY_BOT below the first scallop
under_cut = (
    cq.Workplane("XZ")
    .polyline([(TAB_L, -1.0), (TAB_L, UNDER_Z0), (SCALLOPS[0][2][0] - 0.6, BODY_BOT),
               (BIG, BODY_BOT), (BIG, -1.0)])
    .close()
    .extrude(BIG / 2, both=True)
)
body = body.cut(under_cut)


def scallop_ledge(flip):
    """bead along the lower part of the second scallop wall"""
    cx, cy, r = circle_through(*SCALLOPS[1])
    (x1, y1), _, (x3, y3) = SCALLOPS[1]
    a0 = math.atan2(y1 - cy, x1 - cx)
    a1 = math.atan2(y3 - cy, x3 - cx)
    led = (
        annular_sector(cx, cy, r - LEDGE_W, r + 0.4, a0, a1, flip)
        .extrude(LEDGE_TOP - BODY_BOT)
        .translate((0, 0, BODY_BOT))
    )
    try:
        led = led.faces(">Z").edges(cq.selectors.RadiusNthSelector(0)).fillet(LEDGE_W * 0.8)
    except Exception:
        pass
    return led


base = keel.union(body).union(scallop_ledge(False)).union(scallop_ledge(True))
keel_edges = [
    e for e in base.edges().vals()
    if abs(abs(e.Center().y) - TAB_HW) < 0.05
    and e.BoundingBox().zmin > UNDER_Z0 - 0.1
    and e.BoundingBox().zmax < BODY_BOT + 0.1
    and e.BoundingBox().xmin > TAB_L - 0.1
]
if keel_edges:
    base = base.newObject(keel_edges).fillet(KEEL_FILLET)


# ---------------- arms ----------------
def arm_solid(sign):
    sec = (
        cq.Workplane("XZ")
        .spline(ARM_SECTION, periodic=True)
        .close()
        .extrude(-(ARM_LEN + 5))  # XZ normal is -Y: negative extrude runs toward +Y
    )
    # lobe outline (top view), tangent-continuous so the rim fillet runs all round
    x0 = ARM_X0 - LOBE_CLEAR
    lobe = (
        cq.Workplane("XY")
        .moveTo(x0, ARM_Y0)
        .lineTo(x0, ARM_LEN - LOBE_TIP_R)
        .tangentArcPoint((x0 + LOBE_TIP_R, ARM_LEN), relative=False)
        .lineTo(LOBE_XMAX - LOBE_OUT_R, ARM_LEN)
        .tangentArcPoint((LOBE_XMAX, ARM_LEN - LOBE_OUT_R), relative=False)
        .tangentArcPoint(LOBE_P1, relative=False)
        .tangentArcPoint((LOBE_X_END, ARM_Y0), relative=False)
        .close()
        .extrude(40.0)
    )
    arm = sec.intersect(lobe)
    rim = [e for e in arm.edges().vals()
           if e.geomType() == "BSPLINE" and abs(e.BoundingBox().ymax - ARM_Y0) > 0.01]
    arm = arm.newObject(rim).fillet(ARM_RIM_FILLET)

    # the rim settles down to the body top where the arm meets the saddle:
    # remove everything above a rounded shoulder (arc in YZ, extruded along X)
    def shoulder_z(y):
        return TAPER_CZ + math.sqrt(TAPER_R**2 - (y - TAPER_CY) ** 2)

    y_s = ARM_Y0 - 2.0
    y_m = 0.5 * (y_s + TAPER_CY)
    taper = (
        cq.Workplane("YZ")
        .moveTo(y_s, 40.0)
        .lineTo(y_s, shoulder_z(y_s))
        .threePointArc((y_m, shoulder_z(y_m)), (TAPER_CY, TAPER_CZ + TAPER_R))
        .lineTo(TAPER_CY, 40.0)
        .close()
        .extrude(BIG / 2, both=True)
    )
    arm = arm.cut(taper)
    # soften the edges of the trimmed shoulder (the face of the X-axis cylinder)
    cut_faces = []
    for f in arm.faces().vals():
        if f.geomType() != "CYLINDER":
            continue
        n = f.normalAt(f.Center())
        if abs(n.x) < 1e-3 and n.z > 0.3 and f.BoundingBox().ymax < TAPER_CY:
            cut_faces.append(f)
    if cut_faces:
        soft = [e for e in cut_faces[0].Edges() if abs(e.BoundingBox().ymax - ARM_Y0) > 0.05]
        try:
            arm = arm.newObject(soft).fillet(TAPER_FILLET)
        except Exception:
            pass

    # block under the band (its top is buried inside the band)
    block = (
        cq.Workplane("XZ")
        .polyline([(BLOCK_X0, BODY_BOT), (BLOCK_X1, BODY_BOT), (BLOCK_X1, BLOCK_TOP),
                   (44.0, BLOCK_TOP), (42.4, 14.2), (38.8, 10.9), (BLOCK_X0, 8.2)])
        .close()
        .extrude(-(BLOCK_Y1 - BLOCK_Y0))
        .translate((0, BLOCK_Y0, 0))
    )
    boss = (
        cq.Workplane("XY").circle(BOSS_R).extrude(BOSS_TOP - BOSS_BASE)
        .translate((BOSS_X, BOSS_Y, BOSS_BASE))
    )
    a = arm.union(block).union(boss)
    hole = (
        cq.Workplane("XY").circle(BOSS_HOLE_R).extrude(40.0)
        .translate((BOSS_X, BOSS_Y, -5.0))
    )
    cbore = (
        cq.Workplane("XY").circle(CB_R).extrude(CB_TOP + 1.0)
        .translate((BOSS_X, BOSS_Y, -1.0))
    )
    a = a.cut(hole).cut(cbore)
    if sign < 0:
        a = a.mirror("XZ")
    return a


part = base.union(arm_solid(+1)).union(arm_solid(-1))

# ---------------- saddle cut-out and its lips ----------------
saddle = (
    cq.Workplane("XY").circle(SADDLE_R).extrude(60.0)
    .translate((SADDLE_CX, 0, -10.0))
)
part = part.cut(saddle)

for flip in (False, True):
    # lip angles are measured from the -X direction at the saddle centre
    lip = (
        annular_sector(SADDLE_CX, 0.0, SADDLE_R - LIP_W, SADDLE_R + 0.5,
                       math.pi - math.radians(LIP_A0), math.pi - math.radians(LIP_A1), flip)
        .extrude(LIP_T)
        .translate((0, 0, BODY_TOP - LIP_T))
    )
    part = part.union(lip)

# ---------------- tab cross hole (along Y) ----------------
tab_hole = (
    cq.Workplane("XZ").center(TAB_HOLE_X, TAB_HOLE_Z).circle(TAB_HOLE_R)
    .extrude(30.0, both=True)
)
part = part.cut(tab_hole)

result = part.rotate((0, 0, 0), (0, 1, 0), TILT_DEG)
